import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 100.0          # extrusion height (Z)
W = 70.0           # overall width (X)
L_LEFT = 162.0     # length of the plain -X wall (Y)
L_RIGHT = 157.4    # Y of the back-right corner (back wall is slightly slanted)
T = 4.2            # wall thickness

# moulded +X side, from the front (-Y) end towards the back
FRONT_W = 47.0     # width of the front wall
STEP_Y = 17.9      # Y of the small outward step
STEP_X = 50.2      # X after the step
NOTCH1_Y = 43.3    # top of the stepped section (45 deg V-notch follows)
NOTCH1_D = 2.15    # size of the 45 deg inward jog before the convex face
INNER_NOTCH_DROP = 2.8  # inner V-notch lies this much lower (in X+Y)
INNER_NOTCH_D = 2.3     # step-in of the inner V-notch
CREST_X = 58.9     # max X (crest) of the convex face
CURVE_X1 = 56.4    # X at end of convex face (crease)
NOTCH2_Y = 109.3   # Y at end of convex face (small outward jog follows)
COVE_X = 58.8      # X where the cove starts
COVE_Y = 111.3     # Y where the cove starts
COVE_R = 6.5       # cove (concave) radius
ROUND_R = 7.5      # round (convex) radius
OGEE_ANG = 62.0    # turning angle of cove / round (deg)

# edge treatment (vertical edges)
R_FR = 1.8         # front-right outer corner
R_FL = 2.0         # front-left outer corner
R_BL = 2.0         # back-left outer corner
R_BR = 1.5         # back-right outer corner
R_SMALL = 1.0      # small convex corners of steps
R_CONC = 0.6       # outer concave corners
R_IN = 1.2         # inner corners of the four main walls


def crest_circle(p0, p1, xmax):
    """circle through p0 and p1 whose maximum X (crest) equals xmax"""
    (x0, y0), (x1, y1) = p0, p1

    def cx_of(cy):
        return (xmax ** 2 - x0 ** 2 - (y0 - cy) ** 2) / (2.0 * (xmax - x0))

    def f(cy):
        cx = cx_of(cy)
        return (x1 - cx) ** 2 + (y1 - cy) ** 2 - (xmax - cx) ** 2

    lo, hi = y0, y1
    for _ in range(200):
        mid = 0.5 * (lo + hi)
        if f(lo) * f(mid) <= 0:
            hi = mid
        else:
            lo = mid
    cy = 0.5 * (lo + hi)
    cx = cx_of(cy)
    return cx, cy, xmax - cx


# convex face: one circular arc from the lower V-notch to the upper crease
P_CURVE0 = (STEP_X - NOTCH1_D, NOTCH1_Y + NOTCH1_D)
P_CURVE1 = (CURVE_X1, NOTCH2_Y)
CIRC = crest_circle(P_CURVE0, P_CURVE1, CREST_X)


def profile_wire(diag_c, diag_d):
    """sharp-cornered closed profile.  The 45 deg V-notch at the foot of the
    convex face lies on the line X+Y = diag_c and steps in by diag_d; from
    there a straight lead-in runs tangent onto the convex arc (zero length
    for the outer skin, whose notch ends right on the arc)."""
    cx, cy, r = CIRC
    q = (STEP_X - diag_d, diag_c - STEP_X + diag_d)
    dx, dy = q[0] - cx, q[1] - cy
    d = math.hypot(dx, dy)
    if d - r > 1e-3:
        # upper tangent point from q onto the circle
        t = math.atan2(dy, dx) + math.acos(r / d)
        tp = (cx + r * math.cos(t), cy + r * math.sin(t))
    else:
        tp = None
        t = math.atan2(dy, dx)
    a1 = math.atan2(P_CURVE1[1] - cy, P_CURVE1[0] - cx)
    am = 0.5 * (t + a1)
    curve_mid = (cx + r * math.cos(am), cy + r * math.sin(am))

    th = math.radians(OGEE_ANG)
    # cove (concave), centre outside (+X) the wall
    kx, ky = COVE_X + COVE_R, COVE_Y
    cove_mid = (kx + COVE_R * math.cos(math.pi - th / 2),
                ky + COVE_R * math.sin(math.pi - th / 2))
    cove_end = (kx + COVE_R * math.cos(math.pi - th),
                ky + COVE_R * math.sin(math.pi - th))
    # straight tangent run, then convex round ending tangent at X = W
    d_ang = math.pi / 2 - th
    psi0 = d_ang - math.pi / 2
    rcx = W - ROUND_R
    rs_x = rcx + ROUND_R * math.cos(psi0)
    rs_y = cove_end[1] + (rs_x - cove_end[0]) * math.tan(d_ang)
    rcy = rs_y - ROUND_R * math.sin(psi0)
    round_mid = (rcx + ROUND_R * math.cos(psi0 / 2), rcy + ROUND_R * math.sin(psi0 / 2))
    round_end = (W, rcy)

    wp = (
        cq.Workplane("XY")
        .moveTo(0, 0)
        .lineTo(FRONT_W, 0)
        .lineTo(FRONT_W, STEP_Y)
        .lineTo(STEP_X, STEP_Y)
        .lineTo(STEP_X, diag_c - STEP_X)
        .lineTo(*q)
    )
    if tp is not None:
        wp = wp.lineTo(*tp)
    wp = (
        wp.threePointArc(curve_mid, P_CURVE1)
        .lineTo(COVE_X, COVE_Y)
        .threePointArc(cove_mid, cove_end)
        .lineTo(rs_x, rs_y)
        .threePointArc(round_mid, round_end)
        .lineTo(W, L_RIGHT)
        .lineTo(0, L_LEFT)
        .close()
    )
    return wp.wire().val()


def fillet_at(wire, pts, r):
    vs = []
    for p in pts:
        best = min(wire.Vertices(),
                   key=lambda v: (v.X - p[0]) ** 2 + (v.Y - p[1]) ** 2)
        vs.append(best)
    return wire.fillet2D(r, vs)


sharp = profile_wire(STEP_X + NOTCH1_Y, NOTCH1_D)

# inner boundary: constant wall thickness offset of the outline; the inner
# V-notch sits a little lower (thicker wall at the foot of the convex face)
inner = profile_wire(STEP_X + NOTCH1_Y - INNER_NOTCH_DROP, INNER_NOTCH_D).offset2D(-T, "intersection")[0]
inner = fillet_at(inner, [(T, T), (FRONT_W - T, T), (W - T, L_RIGHT - T),
                          (T, L_LEFT - T)], R_IN)

# outer boundary with rounded vertical edges
outer = fillet_at(sharp, [(FRONT_W, 0)], R_FR)
outer = fillet_at(outer, [(0, 0)], R_FL)
outer = fillet_at(outer, [(0, L_LEFT)], R_BL)
outer = fillet_at(outer, [(W, L_RIGHT)], R_BR)
outer = fillet_at(outer, [(STEP_X, STEP_Y), (STEP_X, NOTCH1_Y), (COVE_X, COVE_Y)], R_SMALL)
outer = fillet_at(outer, [(FRONT_W, STEP_Y), P_CURVE0, P_CURVE1], R_CONC)

profile = cq.Face.makeFromWires(outer, [inner])
tube = cq.Solid.extrudeLinear(profile, cq.Vector(0, 0, H))

result = cq.Workplane("XY").add(tube)

VIEW = {"azimuth": 45, "elevation": 26}
